import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
L = 120.0          # overall width  (X)
W = 98.0           # overall depth  (Y)
H = 43.0           # overall height (Z)
t_side = 6.8       # side wall thickness
t_front = 4.3      # front wall thickness
t_floor = 3.8      # floor thickness
r_out = 1.3        # outer edge round

# front wall holes
hole_d = 22.6
hole_dx = 36.4
hole_z = H / 2.0

# side wall inner ribs
rib_w = 2.8
rib_h = 3.0
rib_top_drop = 5.7
rib_back_gap = 5.9

# floor bars
bar_x_in = 14.5
bar_x_out = 18.9
bar_h = 7.1
bar_y_end = 13.4
bar_wide_x_in = 12.0
bar_wide_len = 8.6

# rear fittings (two lugs + centre block)
fit_y_front = 30.5
fit_y_back = 43.4
slope_deg = 38.5
tab_x_in = 21.6
tab_x_out = 38.5
tab_h = 11.2
tab_r = 3.8
tab_hole_d = 4.4
tab_hole_z = 5.7
blk_half = 15.0
blk_h = 6.9
blk_hole_dx = 7.4
blk_hole_y = 39.5
blk_hole_d = 4.0
ch_w = 6.1
ch_depth = 3.0
boss_d = 4.5
boss_h = 0.5

# ---------------- shell ----------------
body = cq.Workplane("XY").box(L, W, H, centered=(True, True, False))
body = body.edges().fillet(r_out)

cav_len_y = W - t_front + 2.0
cavity = (
    cq.Workplane("XY")
    .box(L - 2 * t_side, cav_len_y, H, centered=(True, False, False))
    .translate((0, -W / 2 + t_front, t_floor))
)
body = body.cut(cavity)

# front holes
for sx in (-1, 1):
    cyl = (
        cq.Workplane("XZ")
        .center(sx * hole_dx, hole_z)
        .circle(hole_d / 2)
        .extrude(-(t_front + 2))
        .translate((0, -W / 2 - 1, 0))
    )
    body = body.cut(cyl)

# side wall ribs
rib_len = W - t_front - rib_back_gap
for sx in (-1, 1):
    xc = sx * (L / 2 - t_side - rib_w / 2)
    rib = (
        cq.Workplane("XY")
        .box(rib_w, rib_len, rib_h, centered=(True, False, False))
        .translate((xc, -W / 2 + t_front, H - rib_top_drop - rib_h))
    )
    body = body.union(rib)

# floor bars (L-shaped footprint, mirrored)
bar_y0 = -W / 2 + t_front
for sx in (-1, 1):
    pts = [
        (bar_x_out, bar_y0),
        (bar_x_out, bar_y_end),
        (bar_x_in, bar_y_end),
        (bar_x_in, bar_y0 + bar_wide_len),
        (bar_wide_x_in, bar_y0 + bar_wide_len),
        (bar_wide_x_in, bar_y0),
    ]
    pts = [(sx * x, y) for x, y in pts]
    bar = (
        cq.Workplane("XY")
        .workplane(offset=t_floor)
        .polyline(pts)
        .close()
        .extrude(bar_h)
    )
    body = body.union(bar)

# ---------------- rear fittings ----------------
tan_s = math.tan(math.radians(slope_deg))
# wedge height: above the tallest fitting but below where the slope meets the back face
big = min(tab_h + 1.0, 0.95 * (fit_y_back - fit_y_front) / tan_s)
# YZ wedge that keeps everything behind the inclined front plane
wedge = (
    cq.Workplane("YZ")
    .polyline(
        [
            (fit_y_front, t_floor - 0.01),
            (fit_y_back, t_floor - 0.01),
            (fit_y_back, t_floor + big),
            (fit_y_front + big * tan_s, t_floor + big),
        ]
    )
    .close()
    .extrude(L / 2, both=True)
)

fit_depth = fit_y_back - fit_y_front
# lugs: rounded-top profile in XZ, extruded along Y, trimmed by the slope
for sx in (-1, 1):
    xc = sx * (tab_x_in + tab_x_out) / 2
    tw = tab_x_out - tab_x_in
    lug = (
        cq.Workplane("XY")
        .box(tw, fit_depth, tab_h, centered=(True, False, False))
        .translate((xc, fit_y_front, t_floor))
        .edges("|Y and >Z")
        .fillet(tab_r)
    )
    lug = lug.intersect(wedge)
    hole = (
        cq.Workplane("XZ")
        .center(xc, t_floor + tab_hole_z)
        .circle(tab_hole_d / 2)
        .extrude(-(fit_depth + 20))
        .translate((0, fit_y_front - 10, 0))
    )
    lug = lug.cut(hole)
    body = body.union(lug)

# centre block with U-channel and two vertical holes
blk = (
    cq.Workplane("XY")
    .box(2 * blk_half, fit_depth, blk_h, centered=(True, False, False))
    .translate((0, fit_y_front, t_floor))
)
blk = blk.intersect(wedge)
ch_zc = t_floor + blk_h - ch_depth + ch_w / 2
chan = (
    cq.Workplane("XZ")
    .center(0, ch_zc)
    .circle(ch_w / 2)
    .extrude(-(fit_depth + 20))
    .translate((0, fit_y_front - 10, 0))
)
chan = chan.union(
    cq.Workplane("XY")
    .box(ch_w, fit_depth + 20, 20, centered=(True, False, False))
    .translate((0, fit_y_front - 10, ch_zc))
)
blk = blk.cut(chan)
body = body.union(blk)

# bosses under the floor and through holes
for sx in (-1, 1):
    boss = (
        cq.Workplane("XY")
        .center(sx * blk_hole_dx, blk_hole_y)
        .circle(boss_d / 2)
        .extrude(boss_h)
        .translate((0, 0, -boss_h))
    )
    body = body.union(boss)
for sx in (-1, 1):
    h = (
        cq.Workplane("XY")
        .center(sx * blk_hole_dx, blk_hole_y)
        .circle(blk_hole_d / 2)
        .extrude(40)
        .translate((0, 0, -5))
    )
    body = body.cut(h)

result = body
